import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 80.0          # overall width  (X)
D = 50.0          # overall depth  (Y)
H = 110.0         # overall height (Z)

T_SIDE = 8.0      # left / right wall thickness
T_BACK = 8.0      # back wall thickness (+Y)
T_FRONT = 6.0     # front wall thickness (-Y)
T_FLOOR = 8.0     # floor thickness (closed bottom)

SLOT_DEPTH = 2.0      # PCB guide slot depth into each side wall
SLOT_WIDTH = 3.3      # slot width along Y
SLOT_OFFSET = 2.7     # distance from inner face of front wall to slot

TEXT_SIZE = 13.2
TEXT_DEPTH = 1.5
TEXT_KIND = "italic"
# (text, world X of line centre, world Z of line centre); text runs top->bottom
TEXT_LINES = (
    ("MK-312WS", -9.0, 54.3),
    ("pcb@bkiff.com", 7.0, 53.3),
)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- body ----------------
body = cq.Workplane("XY").box(W, D, H, centered=(True, True, False))

# cavity (open at the top)
in_w = W - 2 * T_SIDE
in_d = D - T_BACK - T_FRONT
in_cy = (-D / 2 + T_FRONT + D / 2 - T_BACK) / 2.0
cav_h = H - T_FLOOR
cavity = (
    cq.Workplane("XY")
    .workplane(offset=T_FLOOR)
    .center(0, in_cy)
    .rect(in_w, in_d)
    .extrude(cav_h + 1.0)
)
body = body.cut(cavity)

# PCB guide slots in both side walls, running the full cavity depth
slot_cy = -D / 2 + T_FRONT + SLOT_OFFSET + SLOT_WIDTH / 2.0
for sx in (-1, 1):
    sxc = sx * (in_w / 2.0 + SLOT_DEPTH / 2.0 - 0.5)
    slot = (
        cq.Workplane("XY")
        .workplane(offset=T_FLOOR)
        .center(sxc, slot_cy)
        .rect(SLOT_DEPTH + 1.0, SLOT_WIDTH)
        .extrude(cav_h + 1.0)
    )
    body = body.cut(slot)

# ---------------- engraved text on the back face ----------------
# plane on the back face: normal +Y, reading direction downwards (-Z),
# letter tops pointing towards -X
for txt, tx, tz in TEXT_LINES:
    tplane = cq.Plane(origin=(tx, D / 2.0, tz),
                      xDir=(0, 0, -1), normal=(0, 1, 0))
    t = (
        cq.Workplane(tplane)
        .text(txt, TEXT_SIZE, -TEXT_DEPTH, combine=False,
              halign="center", valign="center", font="DejaVu Sans",
              kind=TEXT_KIND)
    )
    body = body.cut(t)

result = body
